import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
DISC_R = 36.6          # base flange radius
DISC_H = 15.6          # base flange thickness

RING_RO = 18.15        # central boss outer radius
RING_RI = 14.85        # central boss bore radius
RING_H = 27.8          # central boss height
FLOOR_Z = 8.3          # floor of the central bore
CENTER_HOLE_R = 7.0    # through hole under the bore

ARM_H = 20.5           # height of the two square arms
ARM_Y_W = 22.1         # width of the +Y arm
ARM_Y_L = 44.9         # length (from hub centre) of the +Y arm
ARM_Y_ANG = 90.0
ARM_L_W = 28.65        # width of the lower-left arm
ARM_L_L = 54.8         # length of the lower-left arm
ARM_L_ANG = 213.6
ARM_BORE_R = 6.8       # socket bore in the arm ends
ARM_BORE_STOP = 27.5   # sockets reach to this distance from the hub centre

TUBE_ANG = -16.0       # tube direction in plan
TUBE_TILT = 5.5        # tube rises outward by this angle
TUBE_R = 18.15
TUBE_BORE_R = 8.45
TUBE_BORE_S = 26.0     # plan distance of the blind end of the tube bore
TUBE_END_S = 62.25     # plan distance of the tube end centre
TUBE_END_Z = 15.5      # height of the tube axis at its end
TUBE_START_S = 15.3    # plan distance of the (vertical) start face of the tube

SADDLE_HALF_W = 16.65  # half width of the web block around the tube root
SADDLE_L = 40.75       # plan length of the web block
SADDLE_H = 27.0        # height of the web block

PIN_R = 0.9            # small cross pin holes
PIN_Y_S = 32.9
PIN_L_S = 38.2
PIN_T_S = 37.75

# flange holes (x, y, radius); the small one just touches the +Y arm side
FLANGE_HOLES = [(0.8, -25.35, 6.55),
                (ARM_Y_W / 2.0 + 5.8 + 0.05, 19.2, 5.8),
                (-21.82, 11.79, 6.6)]

TEXT = "RJL2.6"         # raised lettering on top of the +Y arm
TEXT_SIZE = 5.0
TEXT_H = 0.5
TEXT_POS = (0.55, 26.6)

POCKET_S = 21.5        # rectangular pockets in the underside
POCKET_DEPTH = 4.5
POCKET_T = (7.25, 14.25)   # (along tube, across)
POCKET_L = (8.0, 12.0)     # (along arm, across)


def dirv(ang):
    a = math.radians(ang)
    return (math.cos(a), math.sin(a))


def arm_box(ang, length, width, height, s0=0.0):
    """Box lying on z=0 running radially from s0 to length along angle ang."""
    b = (cq.Workplane("XY")
         .center((s0 + length) / 2.0, 0)
         .rect(length - s0, width)
         .extrude(height))
    return b.rotate((0, 0, 0), (0, 0, 1), ang)


def vcyl(x, y, r, z0, h, seam_ang=45.0):
    """Vertical cylinder; seam_ang only places the parametric seam line."""
    a = math.radians(seam_ang)
    pl = cq.Plane(origin=(x, y, z0), xDir=(math.cos(a), math.sin(a), 0), normal=(0, 0, 1))
    return cq.Workplane(pl).circle(r).extrude(h)


# ---------------- solids ----------------
disc = cq.Workplane("XY").circle(DISC_R).extrude(DISC_H)
ring = cq.Workplane("XY").circle(RING_RO).extrude(RING_H)
arm_y = arm_box(ARM_Y_ANG, ARM_Y_L, ARM_Y_W, ARM_H)
arm_l = arm_box(ARM_L_ANG, ARM_L_L, ARM_L_W, ARM_H)
saddle = arm_box(TUBE_ANG, SADDLE_L, 2 * SADDLE_HALF_W, SADDLE_H)

# tilted tube
ca, sa = dirv(TUBE_ANG)
tilt = math.radians(TUBE_TILT)
d = cq.Vector(math.cos(tilt) * ca, math.cos(tilt) * sa, math.sin(tilt))
p_end = cq.Vector(TUBE_END_S * ca, TUBE_END_S * sa, TUBE_END_Z)
tube_len = (TUBE_END_S - TUBE_START_S + 5.0) / math.cos(tilt)
p_start = p_end - d * tube_len
down = cq.Vector(math.sin(tilt) * ca, math.sin(tilt) * sa, -math.cos(tilt))
tube = cq.Workplane(cq.Plane(origin=p_start, xDir=down, normal=d)).circle(TUBE_R).extrude(tube_len)
# vertical start face of the tube
tube = tube.cut(arm_box(TUBE_ANG, TUBE_START_S, 200.0, 200.0, s0=-100.0).translate((0, 0, -50)))

body = disc.union(ring).union(arm_y).union(arm_l).union(saddle).union(tube)

# flat underside
body = body.cut(cq.Workplane("XY").rect(400, 400).extrude(-100))

# ---------------- cuts ----------------
# central bore and through hole
body = body.cut(vcyl(0, 0, RING_RI, FLOOR_Z, RING_H + 50))
body = body.cut(vcyl(0, 0, CENTER_HOLE_R, -10, 100))

# flange holes
for hx, hy, r in FLANGE_HOLES:
    body = body.cut(vcyl(hx, hy, r, -1, DISC_H + 2))

# sockets in the square arms
for ang, length in ((ARM_Y_ANG, ARM_Y_L), (ARM_L_ANG, ARM_L_L)):
    sock_len = length - ARM_BORE_STOP + 5.0
    pl = cq.Plane(origin=(ARM_BORE_STOP, 0, ARM_H / 2.0), xDir=(0, 0, 1), normal=(1, 0, 0))
    sock = cq.Workplane(pl).circle(ARM_BORE_R).extrude(sock_len)
    body = body.cut(sock.rotate((0, 0, 0), (0, 0, 1), ang))

# tube bore: blind hole from the tube end face
bore_len = (TUBE_END_S - TUBE_BORE_S) / math.cos(tilt)
lat = cq.Vector(-sa, ca, 0)   # plan-lateral direction of the tube (seam placed on its -side)
bore = (cq.Workplane(cq.Plane(origin=p_end - d * bore_len, xDir=-lat, normal=d))
        .circle(TUBE_BORE_R).extrude(bore_len + 5.0))
body = body.cut(bore)

# vertical pin holes through arms / tube
for ang, s in ((ARM_Y_ANG, PIN_Y_S), (ARM_L_ANG, PIN_L_S), (TUBE_ANG, PIN_T_S)):
    cx, cy = dirv(ang)
    body = body.cut(cq.Workplane("XY").center(s * cx, s * cy)
                    .circle(PIN_R).extrude(200).translate((0, 0, -10)))

# rectangular pockets in the underside
for ang, (pl, pw) in ((TUBE_ANG, POCKET_T), (ARM_L_ANG, POCKET_L)):
    pk = (cq.Workplane("XY").center(POCKET_S, 0).rect(pl, pw)
          .extrude(POCKET_DEPTH + 5).translate((0, 0, -5)))
    body = body.cut(pk.rotate((0, 0, 0), (0, 0, 1), ang))

# raised lettering on the +Y arm
try:
    txt = (cq.Workplane("XY").workplane(offset=ARM_H - 0.05)
           .center(*TEXT_POS)
           .text(TEXT, TEXT_SIZE, TEXT_H + 0.05, font="DejaVu Sans", kind="bold",
                 halign="center", valign="center", combine=False))
    body = body.union(txt)
except Exception:
    pass

result = body

VIEW = {"azimuth": 45, "elevation": 26}
